import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
L = 60.0          # overall length  (X)
W = 44.5          # overall depth   (Y)
H = 38.35         # overall height  (Z)
R_V = 0.8         # rounding of the vertical edges
R_TB = 0.6        # rounding of the top / bottom outer edges

# top tray pocket
RIM_X = 7.5       # rim width left/right
RIM_Y = 7.1       # rim width front/back
POCKET_D = 6.8    # pocket depth
CH_H = 1.9        # horizontal size of the pocket-wall bevel
CH_V = 3.7        # vertical size of the pocket-wall bevel

# front vertical channel (full height)
SLOT_W = 20.0
SLOT_D = 9.9
R_SLOT_TOP = 0.6   # rounding of the channel back-wall top edge

# through holes in the pocket floor (diamond pattern)
HOLE_D = 5.9
HOLE_DX = 11.0
HOLE_DY = 7.1

# relief slots in the underside (dead-end slots: two from the sides, two from the back)
GROOVE_H = 7.0    # slot height
GX_W = 3.2        # width of the side slots (centred on y = 0)
GX_END = 19.8     # |x| where the side slots end
GY_W = 3.7        # width of the back slots
GY_C = 7.95       # |x| of the back slot centre lines
GY_END = 12.6     # y where the back slots end
R_MOUTH = 0.5     # rounding of the slot mouth edges

# embossed marking on the back rim
TEXT = "38.9"
TEXT_SIZE = 7.6
TEXT_H = 0.3


# ---------------- body with front channel ----------------
body = cq.Workplane("XY").box(L, W, H, centered=(True, True, False))
slot = (cq.Workplane("XY")
        .center(0, -W / 2 + SLOT_D / 2 - 1.0)
        .rect(SLOT_W, SLOT_D + 2.0)
        .extrude(H + 2).translate((0, 0, -1)))
body = body.cut(slot)

# round the convex vertical edges (outer corners + channel mouth)
y_in = -W / 2 + SLOT_D
body = body.edges(
    cq.selectors.BoxSelector((-L, -W, -1), (L, y_in - 0.5, H + 1))
    & cq.selectors.ParallelDirSelector(cq.Vector(0, 0, 1))
).fillet(R_V)
body = body.edges(
    cq.selectors.BoxSelector((-L, y_in + 0.5, -1), (L, W, H + 1))
    & cq.selectors.ParallelDirSelector(cq.Vector(0, 0, 1))
).fillet(R_V)
# round top and bottom outer edges
body = body.faces(">Z").edges().fillet(R_TB)
body = body.faces("<Z").edges().fillet(R_TB)

# ---------------- top pocket: bevelled upper part + vertical lower part ----
op_x = L - 2 * RIM_X
op_y = W - 2 * RIM_Y
fl_x = op_x - 2 * CH_H
fl_y = op_y - 2 * CH_H
ext = 0.5  # overshoot above the top face
bevel = (cq.Workplane("XY").workplane(offset=H - CH_V)
         .rect(fl_x, fl_y).workplane(offset=CH_V + ext)
         .rect(fl_x + 2 * CH_H * (CH_V + ext) / CH_V,
               fl_y + 2 * CH_H * (CH_V + ext) / CH_V)
         .loft())
lower = (cq.Workplane("XY").workplane(offset=H - POCKET_D)
         .rect(fl_x, fl_y).extrude(POCKET_D - CH_V + 0.01))
body = body.cut(bevel).cut(lower)

# soften the edge where the channel back wall meets the pocket floor
z_fl = H - POCKET_D
body = body.edges(
    cq.selectors.BoxSelector((-SLOT_W / 2 + 0.1, y_in - 0.1, z_fl - 0.1),
                             (SLOT_W / 2 - 0.1, y_in + 0.1, z_fl + 0.1))
).fillet(R_SLOT_TOP)

# ---------------- underside relief slots ----------------
for sx in (-1, 1):
    side = (cq.Workplane("XY").workplane(offset=-1.0)
            .center(sx * (L / 2 + GX_END) / 2 + sx * 0.5, 0)
            .rect(L / 2 - GX_END + 1.0, GX_W)
            .extrude(GROOVE_H + 1.0))
    back = (cq.Workplane("XY").workplane(offset=-1.0)
            .center(sx * GY_C, (W / 2 + GY_END) / 2 + 0.5)
            .rect(GY_W, W / 2 - GY_END + 1.0)
            .extrude(GROOVE_H + 1.0))
    body = body.cut(side).cut(back)

# round the vertical mouth edges of the underside slots
zsel = cq.selectors.ParallelDirSelector(cq.Vector(0, 0, 1))
mouth_sel = None
for sx in (-1, 1):
    for sy in (-1, 1):
        bx = cq.selectors.BoxSelector(
            (sx * L / 2 - 0.3, sy * GX_W / 2 - 0.3, 0.0),
            (sx * L / 2 + 0.3, sy * GX_W / 2 + 0.3, GROOVE_H + 0.1))
        mouth_sel = bx if mouth_sel is None else mouth_sel + bx
        bx = cq.selectors.BoxSelector(
            (sx * GY_C + sy * GY_W / 2 - 0.3, W / 2 - 0.3, 0.0),
            (sx * GY_C + sy * GY_W / 2 + 0.3, W / 2 + 0.3, GROOVE_H + 0.1))
        mouth_sel = mouth_sel + bx
body = body.edges(mouth_sel & zsel).fillet(R_MOUTH)

# ---------------- holes through the pocket floor ----------------
pts = [(0, HOLE_DY), (0, -HOLE_DY), (HOLE_DX, 0), (-HOLE_DX, 0)]
holes = (cq.Workplane("XY").workplane(offset=-1.0)
         .pushPoints(pts).circle(HOLE_D / 2).extrude(H))
body = body.cut(holes)

# ---------------- embossed number on the back rim ----------------
txt = (cq.Workplane("XY").workplane(offset=H)
       .center(0, W / 2 - RIM_Y / 2)
       .transformed(rotate=(0, 0, 180))
       .text(TEXT, TEXT_SIZE, TEXT_H, halign="center", valign="center"))
body = body.union(txt)

result = body

VIEW = {"azimuth": 45, "elevation": 26}
